import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
W = 77.8            # full depth (Y) of the three clamp bars (centred on Y = 0)
PY0, PY1 = -W / 2, 3.4  # Y range of the flexure arms / beam plate (front aligned)

# disc (flange) at the right, front side
DISC_R = 30.0
DISC_T = 15.6           # disc thickness, front face flush with the plate front
DISC_Y0, DISC_Y1 = -W / 2, -W / 2 + DISC_T
DISC_HOLE_OFF = 13.75
DISC_HOLE_D = 10.2
DISC_CB_D = 16.5        # counterbore on the back face of the disc
DISC_CB_DEPTH = 8.0

# right clamp bar
RB_X0, RB_X1 = 26.2, 40.3
RB_H = 14.5             # half height
RB_GROOVE_D = 7.0
RB_GROOVE_H = 3.3       # half height of groove
RB_HOLE_Z = 8.9
PIN_D = 1.2             # small pin hole at the centre of the groove
PIN_DEPTH_IN = 6.0      # how far it runs on into the beam

# bolt holes / nut traps (shared)
HOLE_Y = 15.6
BOLT_D = 6.5
NUT_AF = 11.5
NUT_DEPTH = 6.5

# upper-left clamp bar (local frame, origin = outer top corner)
UB_ORG = (-126.2, 23.6)
UB_ROT = 8.0            # rotation about +Y (deg)
UB_W = 13.2
UB_WIDE_H = 10.5
UB_NARROW_X = 6.2
UB_TOT_H = 19.1
UB_LIP_X = 3.85
UB_LIP_H = 1.6
UB_HOLE_Z = -5.25
ARM_T0, ARM_T1 = 10.35, 16.95   # arm band (distance from outer face of the wide part)

# lower-left clamp bar (local frame, origin = outer bottom corner)
LB_ORG = (-104.1, -24.0)
LB_ROT = -8.7
LB_W = 13.3
LB_WIDE_H = 10.8
LB_NARROW_X = 6.5
LB_TOT_H = 16.9
LB_HOLE_Z = 5.4

# merged beam: V notch between the two arms ends with a flat tip here
NOTCH_X = -77.6

# bosses
BOSS_R = 10.9
BOSS_HOLE_D = 8.3
UBOSS_TOP = (-86.7, 23.4)
UBOSS_DIR = (0.425, -0.906)     # pointing down into the arm
LBOSS_BOT = (-53.6, -22.4)
LBOSS_DIR = (0.447, 0.894)      # pointing up into the beam
UB_CUT_P, UB_CUT_SLOPE = (-79.0, 6.9), -0.10     # upper boss sits on the arm top
LB_CUT_P, LB_CUT_SLOPE = (-47.0, -4.6), 0.096     # lower boss hangs under the beam

# arm windows (nut-trap clearance)
WIN_Y0, WIN_Y1 = -24.0, -7.0
WIN_RECESS = 0.6          # shallow recess in the bar's inner face above/below the window
WIN_LEN = 6.0             # window length along the arm
WIN2_X0, WIN2_X1 = -96.3, -89.8
BEAM_NOTCH_L, BEAM_NOTCH_W = 6.3, 15.6   # beam cut-out in front of the right bar

# marking
TEXT = "300, 300, 60"
TEXT_SIZE = 10.2
TEXT_X, TEXT_Y = -20.4, -17.8
TEXT_DEPTH = 0.8


# ---------------------------------------------------------------- helpers
def rot_xz(p, deg):
    """rotation about +Y applied to an (x, z) point"""
    a = math.radians(deg)
    x, z = p
    return (x * math.cos(a) + z * math.sin(a), -x * math.sin(a) + z * math.cos(a))


def to_global(p, org, deg):
    x, z = rot_xz(p, deg)
    return (org[0] + x, org[1] + z)


def prism(pts, y0, y1):
    """closed XZ polygon extruded from y0 to y1"""
    return (cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close()
            .extrude(y1 - y0))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def hex_prism_x(x0, x1, y, z, af):
    """hexagonal prism along X, flats facing +-Y (vertices at +-Z)"""
    r = af / math.sqrt(3.0)
    pts = [(y + r * math.cos(math.radians(90 + 60 * k)),
            z + r * math.sin(math.radians(90 + 60 * k))) for k in range(6)]
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close()
            .extrude(x1 - x0))


def cyl_x(x0, x1, y, z, d):
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).center(y, z)
            .circle(d / 2.0).extrude(x1 - x0))


def line_y(p, q, x):
    return p[1] + (q[1] - p[1]) * (x - p[0]) / (q[0] - p[0])


# ---------------------------------------------------------------- clamp bars
def upper_bar():
    prof = [(0, 0), (UB_W, 0), (UB_W, -UB_TOT_H), (UB_LIP_X, -UB_TOT_H),
            (UB_LIP_X, -UB_TOT_H + UB_LIP_H), (UB_NARROW_X, -UB_TOT_H + UB_LIP_H),
            (UB_NARROW_X, -UB_WIDE_H), (0, -UB_WIDE_H)]
    b = prism(prof, -W / 2, W / 2)
    for sy in (-HOLE_Y, HOLE_Y):
        b = b.cut(cyl_x(-1, UB_W + 1, sy, UB_HOLE_Z, BOLT_D))
        b = b.cut(hex_prism_x(UB_W - NUT_DEPTH, UB_W + 1, sy, UB_HOLE_Z, NUT_AF))
    return b.rotate((0, 0, 0), (0, 1, 0), UB_ROT).translate((UB_ORG[0], 0, UB_ORG[1]))


def lower_bar():
    prof = [(0, 0), (LB_W, 0), (LB_W, LB_TOT_H), (LB_NARROW_X, LB_TOT_H),
            (LB_NARROW_X, LB_WIDE_H), (0, LB_WIDE_H)]
    b = prism(prof, -W / 2, W / 2)
    for sy in (-HOLE_Y, HOLE_Y):
        b = b.cut(cyl_x(-1, LB_W + 1, sy, LB_HOLE_Z, BOLT_D))
        b = b.cut(hex_prism_x(LB_W - NUT_DEPTH, LB_W + 1, sy, LB_HOLE_Z, NUT_AF))
    return b.rotate((0, 0, 0), (0, 1, 0), LB_ROT).translate((LB_ORG[0], 0, LB_ORG[1]))


def right_bar():
    prof = [(RB_X0, -RB_H), (RB_X1, -RB_H), (RB_X1, -RB_GROOVE_H),
            (RB_X1 - RB_GROOVE_D, -RB_GROOVE_H), (RB_X1 - RB_GROOVE_D, RB_GROOVE_H),
            (RB_X1, RB_GROOVE_H), (RB_X1, RB_H), (RB_X0, RB_H)]
    b = prism(prof, -W / 2, W / 2)
    for sy in (-HOLE_Y, HOLE_Y):
        for sz in (-RB_HOLE_Z, RB_HOLE_Z):
            b = b.cut(cyl_x(RB_X0 - 1, RB_X1 + 1, sy, sz, BOLT_D))
            b = b.cut(hex_prism_x(RB_X0 - 1, RB_X0 + NUT_DEPTH + 1.0, sy, sz, NUT_AF))
    return b


# ---------------------------------------------------------------- arms + beam
def tangent_arc(p, slope, x_end, upward_center):
    """arc leaving p with the given slope and arriving horizontal at x = x_end.
    returns (mid point, end point)"""
    th = math.atan(abs(slope))
    r = (x_end - p[0]) / math.sin(th)
    if upward_center:
        cz = p[1] + r * math.cos(th)
        ang0, ang1 = -math.pi / 2 - th, -math.pi / 2
    else:
        cz = p[1] - r * math.cos(th)
        ang0, ang1 = math.pi / 2 + th, math.pi / 2
    cx = x_end
    am = 0.5 * (ang0 + ang1)
    mid = (cx + r * math.cos(am), cz + r * math.sin(am))
    end = (cx + r * math.cos(ang1), cz + r * math.sin(ang1))
    return mid, end


def flexure_profile(wp):
    """closed XZ outline of the two flexure arms and the merged tapered beam"""
    c_top = to_global((UB_W, -ARM_T0), UB_ORG, UB_ROT)       # upper arm, top edge
    c_bot = to_global((UB_W, -ARM_T1), UB_ORG, UB_ROT)       # upper arm, bottom edge
    u_dir = rot_xz((1.0, 0.0), UB_ROT)
    p_bot = to_global((LB_W, ARM_T0), LB_ORG, LB_ROT)        # lower arm, bottom edge
    p_top = to_global((LB_W, LB_TOT_H), LB_ORG, LB_ROT)      # lower arm, top edge
    l_dir = rot_xz((1.0, 0.0), LB_ROT)

    # beam edges: single large arcs, tangent to the arms, horizontal at the right bar
    t_mid, t_end = tangent_arc(c_top, u_dir[1] / u_dir[0], RB_X0, True)
    b_mid, b_end = tangent_arc(p_bot, l_dir[1] / l_dir[0], RB_X0, False)

    u1 = to_global((10.0, -ARM_T0), UB_ORG, UB_ROT)
    u2 = to_global((10.0, -ARM_T1), UB_ORG, UB_ROT)
    l1 = to_global((10.0, ARM_T0), LB_ORG, LB_ROT)
    l2 = to_global((8.0, LB_TOT_H), LB_ORG, LB_ROT)

    # notch tip between the arms
    n1 = (NOTCH_X, line_y(c_bot, (c_bot[0] + u_dir[0], c_bot[1] + u_dir[1]), NOTCH_X))
    n2 = (NOTCH_X, line_y(p_top, (p_top[0] + l_dir[0], p_top[1] + l_dir[1]), NOTCH_X))

    xr = RB_X0 + 1.5
    return (wp.moveTo(xr, t_end[1])
            .lineTo(*t_end)
            .threePointArc(t_mid, c_top)
            .lineTo(*u1).lineTo(*u2).lineTo(*n1)
            .lineTo(*n2)
            .lineTo(*l2).lineTo(*l1).lineTo(*p_bot)
            .threePointArc(b_mid, b_end)
            .lineTo(xr, b_end[1])
            .close())


def arms_and_beam():
    wp = cq.Workplane("XZ", origin=(0, PY1, 0))
    return flexure_profile(wp).extrude(PY1 - PY0)


def flexure_core(inset):
    """the flexure body shrunk by inset (used to limit the engraving depth)"""
    wp = cq.Workplane("XZ", origin=(0, PY1 + 5, 0))
    return flexure_profile(wp).offset2D(-inset).extrude(PY1 - PY0 + 10)


# ---------------------------------------------------------------- disc
def disc():
    d = (cq.Workplane("XZ", origin=(0, DISC_Y1, 0)).circle(DISC_R)
         .extrude(DISC_Y1 - DISC_Y0))
    pts = [(sx * DISC_HOLE_OFF, sz * DISC_HOLE_OFF) for sx in (-1, 1) for sz in (-1, 1)]
    holes = (cq.Workplane("XZ", origin=(0, DISC_Y1 + 1, 0)).pushPoints(pts)
             .circle(DISC_HOLE_D / 2.0).extrude(DISC_Y1 - DISC_Y0 + 2))
    cbores = (cq.Workplane("XZ", origin=(0, DISC_Y1 + 1, 0)).pushPoints(pts)
              .circle(DISC_CB_D / 2.0).extrude(DISC_CB_DEPTH + 1))
    return d.cut(holes).cut(cbores)


# ---------------------------------------------------------------- bosses
def halfspace_cut(solid, p, slope, keep_above):
    """remove the material on one side of the XZ line through p with given slope"""
    big = 300.0
    ang = math.degrees(math.atan(slope))
    off = -big / 2 if keep_above else big / 2
    cutter = (cq.Workplane("XY").box(big, big, big).translate((0, 0, off))
              .rotate((0, 0, 0), (0, 1, 0), -ang).translate((p[0], 0, p[1])))
    return solid.cut(cutter)


def boss(end, direction, length, hole_depth):
    """round boss with a blind bore, growing from its free end face along direction"""
    ex, ez = end
    dx, dz = direction
    n = math.hypot(dx, dz)
    dx, dz = dx / n, dz / n
    # seam of the cylindrical face placed on the -X side (least visible)
    sx, sz = (-dz, dx) if -dz < 0 else (dz, -dx)   # perpendicular with x < 0
    pl = cq.Plane(origin=(ex, 0, ez), xDir=(sx, 0, sz), normal=(dx, 0, dz))
    b = cq.Workplane(pl).circle(BOSS_R).extrude(length)
    bore = cq.Workplane(pl).workplane(offset=-1.0).circle(BOSS_HOLE_D / 2.0).extrude(hole_depth + 1.0)
    return b, bore


# ---------------------------------------------------------------- assemble
body = arms_and_beam()
body = body.union(upper_bar()).union(lower_bar()).union(right_bar()).union(disc())

# upper boss: stands on the upper flexure arm (ends just below its top surface)
ub, ub_bore = boss(UBOSS_TOP, UBOSS_DIR, 24.0, 16.0)
ub = halfspace_cut(ub, UB_CUT_P, UB_CUT_SLOPE, keep_above=True)
# lower boss: hangs under the merged beam
lb, lb_bore = boss(LBOSS_BOT, LBOSS_DIR, 28.0, 14.0)
lb = halfspace_cut(lb, LB_CUT_P, LB_CUT_SLOPE, keep_above=False)
body = body.union(ub).union(lb).cut(ub_bore).cut(lb_bore)

# clearance windows in the arms in front of the nut traps
w1 = (box(UB_W - WIN_RECESS, UB_W + WIN_LEN, WIN_Y0, WIN_Y1, -ARM_T1 - 3.0, 1.0)
      .rotate((0, 0, 0), (0, 1, 0), UB_ROT).translate((UB_ORG[0], 0, UB_ORG[1])))
w3 = (box(LB_W - WIN_RECESS, LB_W + WIN_LEN, WIN_Y0, WIN_Y1, -1.0, LB_TOT_H + 3.0)
      .rotate((0, 0, 0), (0, 1, 0), LB_ROT).translate((LB_ORG[0], 0, LB_ORG[1])))
body = body.cut(w1).cut(w3)
body = body.cut(box(WIN2_X0, WIN2_X1, WIN_Y0, WIN_Y1, 0.0, 12.0))
# small locating pin hole in the groove floor, running on into the beam
body = body.cut(cyl_x(RB_X0 - PIN_DEPTH_IN, RB_X1 + 1, 0, 0, PIN_D))
# notch in the beam behind the disc in front of the right bar nut traps
body = body.cut(box(RB_X0 - BEAM_NOTCH_L, RB_X0, -HOLE_Y - BEAM_NOTCH_W / 2,
                    -HOLE_Y + BEAM_NOTCH_W / 2, -8.0, 8.0))

# marking text engraved into the top and bottom faces of the beam (reads from below)
try:
    txt_plane = cq.Plane(origin=(TEXT_X, TEXT_Y, 12.0), xDir=(-1, 0, 0), normal=(0, 0, -1))
    txt = cq.Workplane(txt_plane).text(TEXT, TEXT_SIZE, 24.0, combine=False,
                                       halign="center", valign="center")
    txt = txt.cut(flexure_core(TEXT_DEPTH))
    engraved = body.cut(txt)
    if engraved.val().isValid() and len(engraved.solids().vals()) == 1:
        body = engraved
except Exception:
    pass

result = body
